import cadquery as cq
import math
from cadquery.occ_impl.shapes import BRepFilletAPI_MakeChamfer

# ---------------- driving dimensions (mm) ----------------
W = 60.0          # overall X (incl. ledge)
L = 116.0         # overall Y
H = 95.0          # overall Z
X0 = -W / 2       # ledge outer face
X1 = W / 2        # +X face
Y0 = -L / 2
Y1 = L / 2

X_PLATE = -26.3   # -X edge of top plates / middle overhang
X_WEB = -18.0     # -X face of the core (recessed side)
Z_FLOOR = 26.3    # top of bottom block / pocket floors
Z_CEIL = 81.5     # underside of top plates / pocket ceilings
Z_MID = 90.0      # top of middle section
Y_T = 24.0        # tower plate inner edge (at Z=H)
Y_C = 19.0        # chamfer foot on middle top
R_PX = 10.0       # +X vertical corner radius
R_LEDGE = 6.0     # ledge corner radius
CH = 4.0          # chamfer on horizontal edges of pocket / recess openings
CH_V = 2.8        # chamfer on vertical edges of the openings

R_POCKET = 25.0   # front bore radius (concentric with the R_PX corner round)
R_LEDGE_TOP = 4.0

# back tower pocket: chamber X<BP_X_IN, BP_Y_IN[0]<Y<BP_Y_IN[1];
# mouth on the +Y face for X<BP_X_MOUTH
BP_X_IN = 14.2
BP_Y_IN = (28.5, 44.2)
BP_X_MOUTH = 1.2
# back tower window from +X face into the chamber
WIN_Y = (25.5, 38.5)

# middle box (open to +X)
BOX_X = -11.0
BOX_Y = (-18.0, 22.5)
BOX_Z = (35.5, 76.0)
# notch from the top into the box
NOTCH_X = 8.6
NOTCH_Y = (-10.0, 14.2)
CH_NOTCH = 2.2

# engraved letter "L" on the -X face (stroke at +Y side, foot towards -Y)
L_Y = (-3.5, -29.5)
L_Z = (32.5, 73.0)
L_TV = 8.0        # stroke width
L_TH = 5.5        # foot height
L_DEPTH = 0.8

# holes
HOLE_D = 10.0
CB_D = 20.0
CB_DEPTH = 3.0
HOLE_F = (13.5, -42.6)
HOLE_B = (-12.2, 45.7)
HOLE_MID = (-1.8, 3.0)
HOLE_BOX = (19.0, 3.0)

# bottom channel (open to +X and bottom)
CHN_Y = (-22.0, 26.3)
CHN_Z = 26.4
CHN_C = 7.0
FLARE = 4.0       # 45 deg flare of the pocket mouth (plan view)
TAP_X = -6.0      # back end of the tapered guide pocket
TAP_Y = (-10.6, 12.6)
ROOF_Z0 = 6.5     # sloped roof: z = ROOF_Z0 + ROOF_K * x
ROOF_K = 0.65
BORE_D = 18.0     # bore from below around the floor hole
BORE_Z = 24.0


def box(x0, x1, y0, y1, z0, z1):
    """axis-aligned box from min/max coordinates"""
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


def rounded_prism(x0, x1, y0, y1, z0, z1, r_px, r_nx):
    """box with rounded vertical edges: r_px on the +X side, r_nx on the -X side"""
    b = box(x0, x1, y0, y1, z0, z1)
    if r_px > 0:
        b = b.edges("|Z and >X").fillet(r_px)
    if r_nx > 0:
        b = b.edges("|Z and <X").fillet(r_nx)
    return b


# ---------------- main body ----------------
base = rounded_prism(X_WEB, X1, Y0, Y1, 0, Z_FLOOR, R_PX, 0)
core = rounded_prism(X_WEB, X1, Y0, Y1, 0, Z_MID, R_PX, 0)

# top plates + middle overhang, profile in YZ, extruded along X
top_prof = (cq.Workplane("YZ", origin=(X_PLATE, 0, 0))
            .polyline([(Y0, Z_CEIL), (Y0, H), (-Y_T, H), (-Y_C, Z_MID),
                       (Y_C, Z_MID), (Y_T, H), (Y1, H), (Y1, Z_CEIL)]).close()
            .extrude(X1 - X_PLATE))
top_clip = rounded_prism(X_PLATE, X1, Y0, Y1, Z_CEIL - 1, H + 1, R_PX, 0)
top = top_prof.intersect(top_clip)

body = base.union(core).union(top)

# front tower corner pocket (+X,-Y): vertical bore concentric with the corner round
pf = (cq.Workplane("XY", origin=(X1 - R_PX, Y0 + R_PX, Z_FLOOR)).circle(R_POCKET)
      .extrude(Z_CEIL - Z_FLOOR))
body = body.cut(pf)

# back tower pocket (-X,+Y): inner chamber + mouth on the +Y face,
# open to the recessed -X side
body = body.cut(box(X0 - 1, BP_X_IN, BP_Y_IN[0], BP_Y_IN[1], Z_FLOOR, Z_CEIL))
body = body.cut(box(X0 - 1, BP_X_MOUTH, BP_Y_IN[1] - 0.01, Y1 + 1, Z_FLOOR, Z_CEIL))

# back tower window from the +X face into the chamber
body = body.cut(box(BP_X_IN - 0.5, X1 + 1, WIN_Y[0], WIN_Y[1], Z_FLOOR, Z_CEIL))

# ---------------- chamfered frames around the openings ----------------
_EPS = 0.05


def _near(a, b):
    return abs(a - b) < _EPS


def _pts(e):
    return [e.positionAt(t) for t in (0.0, 0.25, 0.5, 0.75, 1.0)]


def _on_fr_corner(p):
    cx, cy = X1 - R_PX, Y0 + R_PX
    return (_near(math.hypot(p.x - cx, p.y - cy), R_PX)
            and p.x > cx - _EPS and p.y < cy + _EPS)


def _frame_edge(e):
    P = _pts(e)
    if not all(Z_FLOOR - _EPS <= p.z <= Z_CEIL + _EPS for p in P):
        return False
    # front pocket loop (front face, corner, +X face)
    if all((_near(p.y, Y0) and p.x > X_WEB + 1) or (_near(p.x, X1) and p.y < -20)
           or _on_fr_corner(p) for p in P):
        return True
    # front face recess: plate underside edge + web edge (full height)
    if all(_near(p.y, Y0) and X_PLATE - _EPS <= p.x <= X_WEB + _EPS for p in P):
        return True
    # back face opening
    if all(_near(p.y, Y1) and p.x > X_WEB - _EPS for p in P):
        return True
    if all(_near(p.y, Y1) and _near(p.z, Z_CEIL) for p in P):
        return True
    # window on +X face (top, bottom and +Y edges; the -Y edge stays sharp)
    if all(_near(p.x, X1) and WIN_Y[0] - _EPS <= p.y <= WIN_Y[1] + _EPS for p in P) \
            and not all(_near(p.y, WIN_Y[0]) for p in P):
        return True
    # back pocket edge on the recessed -X face
    if all(_near(p.x, X_WEB) and _near(p.y, BP_Y_IN[0]) for p in P):
        return True
    return False


def _web_edge(e):
    P = _pts(e)
    return all(_near(p.y, Y0) and _near(p.x, X_WEB) for p in P)


def _is_vertical(e):
    P = _pts(e)
    return all(_near(p.x, P[0].x) and _near(p.y, P[0].y) for p in P)


def chamfer_var(shape, edges_dists):
    """symmetric chamfers with an individual distance per edge"""
    mk = BRepFilletAPI_MakeChamfer(shape.wrapped)
    for e, d in edges_dists:
        mk.Add(d, e.wrapped)
    mk.Build()
    return cq.Shape.cast(mk.Shape())


shp = body.val()
sel = [(e, CH_V if _is_vertical(e) else CH)
       for e in shp.Edges() if _frame_edge(e) or _web_edge(e)]
shp = chamfer_var(shp, sel)
body = cq.Workplane("XY").add(shp)

# ---------------- ledge on the -X side with rounded top edge ----------------
ledge = rounded_prism(X0, X_WEB + 5, Y0, Y1, 0, Z_FLOOR, 0, R_LEDGE)
ledge = ledge.faces(">Z").edges("not >X").fillet(R_LEDGE_TOP)
body = body.union(ledge)

# ---------------- middle section ----------------
body = body.cut(box(BOX_X, X1 + 1, BOX_Y[0], BOX_Y[1], BOX_Z[0], BOX_Z[1]))
body = body.cut(box(NOTCH_X, X1 + 1, NOTCH_Y[0], NOTCH_Y[1], BOX_Z[1] - 1, H + 1))
# small chamfers on the notch's vertical edges at the +X face
shp = body.val()
sel = [e for e in shp.Edges()
       if all(_near(p.x, X1) and (_near(p.y, NOTCH_Y[0]) or _near(p.y, NOTCH_Y[1]))
              and p.z > BOX_Z[1] - _EPS for p in _pts(e))]
if sel:
    shp = shp.chamfer(CH_NOTCH, None, sel)
body = cq.Workplane("XY").add(shp)

# engraved "L" on the recessed -X face
L_letter = (cq.Workplane("YZ", origin=(X_WEB - 1, 0, 0))
            .polyline([(L_Y[0], L_Z[0]), (L_Y[0], L_Z[1]), (L_Y[0] - L_TV, L_Z[1]),
                       (L_Y[0] - L_TV, L_Z[0] + L_TH), (L_Y[1], L_Z[0] + L_TH),
                       (L_Y[1], L_Z[0])]).close()
            .extrude(1 + L_DEPTH))
body = body.cut(L_letter)

# bottom guide pocket (open to +X and below): tapered plan, sloped roof,
# chamfered top corners at the +X face
chn = (cq.Workplane("YZ", origin=(TAP_X - 12, 0, 0))
       .polyline([(CHN_Y[0], -1), (CHN_Y[0], CHN_Z - CHN_C), (CHN_Y[0] + CHN_C, CHN_Z),
                  (CHN_Y[1] - CHN_C, CHN_Z), (CHN_Y[1], CHN_Z - CHN_C), (CHN_Y[1], -1)])
       .close().extrude(X1 + 13 - TAP_X))
taper = (cq.Workplane("XY", origin=(0, 0, -1))
         .polyline([(X1 + 1, CHN_Y[0] - 1), (X1 + 1, CHN_Y[1] + 1),
                    (X1 - FLARE, CHN_Y[1] - FLARE), (TAP_X, TAP_Y[1]),
                    (TAP_X, TAP_Y[0]), (X1 - FLARE, CHN_Y[0] + FLARE)]).close()
         .extrude(CHN_Z + 2))


def _roof_z(x):
    return ROOF_Z0 + ROOF_K * x


roof = (cq.Workplane("XZ", origin=(0, Y1 + 1, 0))
        .polyline([(TAP_X - 15, -5), (X1 + 5, -5),
                   (X1 + 5, _roof_z(X1 + 5)), (TAP_X - 15, _roof_z(TAP_X - 15))]).close()
        .extrude(L + 2))
body = body.cut(taper.intersect(roof).intersect(chn))
# vertical bores from below around the two middle through-holes
for (hx, hy) in (HOLE_BOX, HOLE_MID):
    body = body.cut(cq.Workplane("XY", origin=(hx, hy, -1))
                    .circle(BORE_D / 2).extrude(BORE_Z + 1))

# ---------------- holes ----------------
for (hx, hy) in (HOLE_F, HOLE_B):
    body = body.cut(cq.Workplane("XY", origin=(hx, hy, -1)).circle(HOLE_D / 2).extrude(H + 2))
    body = body.cut(cq.Workplane("XY", origin=(hx, hy, H - CB_DEPTH)).circle(CB_D / 2).extrude(CB_DEPTH + 1))
body = body.cut(cq.Workplane("XY", origin=(HOLE_MID[0], HOLE_MID[1], -1))
                .circle(HOLE_D / 2).extrude(H + 2))
body = body.cut(cq.Workplane("XY", origin=(HOLE_BOX[0], HOLE_BOX[1], -1))
                .circle(HOLE_D / 2).extrude(BOX_Z[0] + 2))

result = body
